import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
# X: from the hex-nut flat (-X) to the outer face of the thin plate (+X)
# Y: symmetric about 0, Z: up from the bottom plane
W = 70.0            # full Y width of back wall / columns / ledge
H = 53.6            # height of back wall and columns

WALL_X0 = 23.6      # back face of the thin part of the back wall
WALL_X1 = 27.6      # front (+X) face of the back wall
BEV_X = 0.8         # shallow bevel around the wall front face
BEV_YZ = 2.0
OUT_CH = 0.6        # small 45 deg chamfer on the outer edge

COL_W = 16.3        # Y width of each column
COL_X_TOP = 11.0    # column back face at the top (head)
COL_X_BOT = 16.0    # column / lower body back face lower down
COL_SL_Z0 = 28.0    # slope start (bottom)
COL_SL_Z1 = 46.7    # slope end (top)
COL_HOLE_X = 19.2
COL_HOLE_Y = 26.6
COL_HOLE_D = 10.0
COL_HOLE_DEPTH = 14.0

LOWER_Z = 34.0      # top of lower back body between the columns
U_RY = 9.0          # elliptical rounding at bottom of U cut
U_RZ = 16.0

# hex post and tapered hex nut behind the back wall
POST_CX = 14.2
POST_R = 8.7        # circumradius
POST_Z0 = 6.3
POST_HOLE_D = 7.0
NUT_CX = 9.6
NUT_R_BOT = 8.6     # nut is a hex frustum, wider at the top
NUT_R_TOP = 11.0
NUT_H = 6.3
RECESS_X1 = 20.7    # recess in the lower body around the nut
RECESS_HW = 9.5

# ledge in front of the wall
LEDGE_X1 = 40.2
LEDGE_Z = 16.6
LEDGE_R = 4.7
LEDGE_TOP_R = 1.0   # soft top edge of the ledge
LEDGE_R2 = 4.5      # concave blend into the floor side
LEDGE_HOLE_X = 32.8
LEDGE_HOLE_Y = 25.8
LEDGE_HOLE_D = 9.0

# floor / channel
FLOOR_W = 51.0
FLOOR_Z = 12.9
SHELF_CH = 0.8
BOT_EDGE_CH = 0.8   # small bevel along the bottom outline of wall block and ledge
TROUGH_Z = 7.5
TROUGH_HW = 20.5    # half width of the trough at the shelf level
TROUGH_FLAT = 17.0  # half width of the flat trough bottom
RAISED_X0 = 72.0
RAISED_Z = 16.2
BOT_CH_Y = 6.1      # rounded bevel along the lower long edges
BOT_CH_Z = 8.4
BOT_BULGE = 0.3

SLOT_W = 5.6
SLOT_R = 1.0
SLOT_X = [(40.4, 53.2), (58.5, 71.6)]
CEN_HOLE_X = 55.6
CEN_HOLE_Y = 8.3
CEN_HOLE_D = 6.0
CEN_CSK_D = 12.0
GROOVE_Y = [5.0, 7.2, 9.4, 11.5, 13.7]
GROOVE_W = 0.45
GROOVE_DEPTH = 1.0
TAB_X = (53.3, 58.3)
TAB_Y_IN = 19.0
TAB_CH = 0.6

# feet (bosses with pockets) under the raised part
FOOT_X = [78.0, 89.5]
FOOT_Y = [-17.0, 0.0, 17.0]
FOOT_R = 6.6
FOOT_H = 8.0
POCKET_D = 9.4
POCKET_DEPTH = 3.0

# thin front plate
PLATE_X0 = 92.0
PLATE_X1 = 96.3
PLATE_TOP = 51.5
PLATE_ARC_R = 7.1   # top corners: arc tangent to the top edge above the upper holes
PLATE_ARC_END = 46.0  # deg, where the 45 deg flank starts
PLATE_HW = 22.4
PLATE_STEP_Z = 17.6
PLATE_CH = 0.6

# hole pattern shared by back wall and plate
HOLE_Y = 13.45
HOLE_Z = [21.5, 46.2]
HOLE_D = 4.0
CSK_D = 9.4         # shallow conical recess on the plate outer face
CSK_D2 = 6.6
CSK_DEPTH = 1.5
WALL_HOLE_D = 5.0
CB_D = 11.0         # counterbore on the back of the lower body
CB_DEPTH = 4.0

hw = W / 2.0
fw = FLOOR_W / 2.0


def hexagon(cx, cy, r):
    """Regular hexagon with flats facing +/-X (vertices on +/-Y)."""
    return [(cx + r * math.cos(math.radians(a)), cy + r * math.sin(math.radians(a)))
            for a in (30, 90, 150, 210, 270, 330)]


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def bottom_edge_profile(s):
    """YZ region removed along a lower long edge (rounded bevel), side s=+1/-1."""
    y_out = fw + 0.05
    p0 = (s * fw, BOT_CH_Z)
    p1 = (s * (fw - BOT_CH_Y), 0.0)
    cy, cz = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    dy, dz = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dy, dz)
    ny, nz = dz / L, -dy / L        # perpendicular
    if ny * s < 0:
        ny, nz = -ny, -nz
    mid = (cy + ny * BOT_BULGE, cz + nz * BOT_BULGE)
    return p0, mid, p1, y_out


# ---------------------------------------------------------------- back block
prof = [
    (COL_X_BOT, 0.0),
    (WALL_X1, 0.0),
    (WALL_X1, H - BEV_YZ - OUT_CH),
    (WALL_X1 - BEV_X, H - OUT_CH),
    (WALL_X1 - BEV_X - OUT_CH, H),
    (COL_X_TOP, H),
    (COL_X_TOP, COL_SL_Z1),
    (COL_X_BOT, COL_SL_Z0),
]
back = (cq.Workplane("XZ").polyline(prof).close()
        .extrude(hw, both=True))
back = back.faces("<Z").edges("|X").chamfer(BOT_EDGE_CH)

# U cut between the columns with elliptical rounding at the bottom
u_hw = hw - COL_W
ucut = (cq.Workplane("YZ").moveTo(-u_hw, H + 5).lineTo(-u_hw, LOWER_Z + U_RZ)
        .ellipseArc(U_RY, U_RZ, 180, 270, startAtCurrent=True)
        .lineTo(u_hw - U_RY, LOWER_Z)
        .ellipseArc(U_RY, U_RZ, 270, 360, startAtCurrent=True)
        .lineTo(u_hw, H + 5).close()
        .extrude(WALL_X0 + 5.0).translate((-5.0, 0, 0)))
back = back.cut(ucut)

# bevel + outer chamfer on the vertical side edges of the wall front face
for s in (1, -1):
    pts = [
        (WALL_X1 + 0.05, s * (hw + 0.05)),
        (WALL_X1 + 0.05, s * (hw - BEV_YZ - OUT_CH)),
        (WALL_X1, s * (hw - BEV_YZ - OUT_CH)),
        (WALL_X1 - BEV_X, s * (hw - OUT_CH)),
        (WALL_X1 - BEV_X - OUT_CH, s * hw),
        (WALL_X1 - BEV_X - OUT_CH, s * (hw + 0.05)),
    ]
    tri = (cq.Workplane("XY").polyline(pts).close()
           .extrude(H + 2).translate((0, 0, LEDGE_Z)))
    back = back.cut(tri)

# column counterbores (blind, from top)
for s in (1, -1):
    back = back.cut(
        cq.Workplane("XY").circle(COL_HOLE_D / 2).extrude(COL_HOLE_DEPTH + 1)
        .translate((COL_HOLE_X, s * COL_HOLE_Y, H - COL_HOLE_DEPTH)))
    back = back.cut(cq.Workplane("XY").add(
        cq.Solid.makeCone(COL_HOLE_D / 2, COL_HOLE_D / 2 + 0.6, 0.6,
                          pnt=cq.Vector(COL_HOLE_X, s * COL_HOLE_Y, H - 0.6),
                          dir=cq.Vector(0, 0, 1))))

# ---------------------------------------------------------------- hex post + nut
post = (cq.Workplane("XY").polyline(hexagon(POST_CX, 0, POST_R)).close()
        .extrude(LOWER_Z - POST_Z0).translate((0, 0, POST_Z0)))
# hex frustum: drawn at the top, extruded downward with an inward taper
nut_taper = math.degrees(math.atan((NUT_R_TOP - NUT_R_BOT) * math.cos(math.radians(30)) / NUT_H))
nut = (cq.Workplane(cq.Plane(origin=(0, 0, NUT_H), xDir=(1, 0, 0), normal=(0, 0, -1)))
       .polyline(hexagon(NUT_CX, 0, NUT_R_TOP)).close()
       .extrude(NUT_H, taper=nut_taper))
back = back.cut(box(COL_X_BOT - 1.0, RECESS_X1, -RECESS_HW, RECESS_HW, -1.0, NUT_H))
back = back.union(post).union(nut)
back = back.cut(
    cq.Workplane("XY").circle(POST_HOLE_D / 2).extrude(20.0)
    .translate((POST_CX, 0, LOWER_Z - 20.0)))
back = back.cut(cq.Workplane("XY").add(
    cq.Solid.makeCone(POST_HOLE_D / 2, POST_HOLE_D / 2 + 1.0, 1.0,
                      pnt=cq.Vector(POST_CX, 0, LOWER_Z - 1.0), dir=cq.Vector(0, 0, 1))))

# ---------------------------------------------------------------- ledge + floor footprint
x_in = WALL_X1 - 1.0
fp = (cq.Workplane("XY")
      .moveTo(x_in, -hw)
      .lineTo(LEDGE_X1 - LEDGE_R, -hw)
      .radiusArc((LEDGE_X1, -hw + LEDGE_R), -LEDGE_R)
      .lineTo(LEDGE_X1, -fw - LEDGE_R2)
      .radiusArc((LEDGE_X1 + LEDGE_R2, -fw), LEDGE_R2)
      .lineTo(PLATE_X0 + 0.5, -fw)
      .lineTo(PLATE_X0 + 0.5, fw)
      .lineTo(LEDGE_X1 + LEDGE_R2, fw)
      .radiusArc((LEDGE_X1, fw + LEDGE_R2), LEDGE_R2)
      .lineTo(LEDGE_X1, hw - LEDGE_R)
      .radiusArc((LEDGE_X1 - LEDGE_R, hw), -LEDGE_R)
      .lineTo(x_in, hw)
      .close())
base = fp.extrude(FLOOR_Z)
base = base.faces(">Z").edges().chamfer(SHELF_CH)     # small bevel on the shelf edges
base = base.faces("<Z").edges().chamfer(BOT_EDGE_CH)  # small bevel on the bottom outline

ledge = (box(x_in, LEDGE_X1, -hw, hw, 0, LEDGE_Z)
         .edges("|Z and >X").fillet(LEDGE_R)
         .faces(">Z").edges("not <X").fillet(LEDGE_TOP_R)
         .faces("<Z").edges("not <X").chamfer(BOT_EDGE_CH))
base = base.union(ledge)
base = base.union(box(RAISED_X0, PLATE_X0 + 0.5, -fw, fw, 0, RAISED_Z))

# ---------------------------------------------------------------- front plate
p0, mid, p1, _ = bottom_edge_profile(1)


def plate_profile(wp):
    # top corners: arc tangent to the top edge (centred above the hole column), then a flank
    cz = PLATE_TOP - PLATE_ARC_R
    a_e = math.radians(PLATE_ARC_END)
    a_m = math.radians((90.0 + PLATE_ARC_END) / 2)
    e = (HOLE_Y + PLATE_ARC_R * math.cos(a_e), cz + PLATE_ARC_R * math.sin(a_e))
    m = (HOLE_Y + PLATE_ARC_R * math.cos(a_m), cz + PLATE_ARC_R * math.sin(a_m))
    flank_z = e[1] - (PLATE_HW - e[0]) / math.tan(a_e)
    top = PLATE_TOP
    return (wp.moveTo(-HOLE_Y, top)
            .lineTo(HOLE_Y, top)
            .threePointArc(m, e)
            .lineTo(PLATE_HW, flank_z)
            .lineTo(PLATE_HW, PLATE_STEP_Z)
            .lineTo(fw, PLATE_STEP_Z - (fw - PLATE_HW))
            .lineTo(fw, BOT_CH_Z)
            .threePointArc(mid, p1)
            .lineTo(-p1[0], 0.0)
            .threePointArc((-mid[0], mid[1]), (-fw, BOT_CH_Z))
            .lineTo(-fw, PLATE_STEP_Z - (fw - PLATE_HW))
            .lineTo(-PLATE_HW, PLATE_STEP_Z)
            .lineTo(-PLATE_HW, flank_z)
            .lineTo(-e[0], e[1])
            .threePointArc((-m[0], m[1]), (-HOLE_Y, top))
            .close())


# plate body plus a 45 deg tapered cap = chamfer around the outer face
plate = plate_profile(cq.Workplane("YZ", origin=(PLATE_X0 + PLATE_CH, 0, 0))).extrude(
    PLATE_X1 - PLATE_X0 - 2 * PLATE_CH)
plate = plate.union(plate_profile(cq.Workplane("YZ", origin=(PLATE_X1 - PLATE_CH, 0, 0)))
                    .extrude(PLATE_CH, taper=45))
plate = plate.union(plate_profile(cq.Workplane("YZ", origin=(PLATE_X0 + PLATE_CH, 0, 0)))
                    .extrude(-PLATE_CH, taper=45))

body = back.union(base).union(plate)

# ---------------------------------------------------------------- trough in the floor
t_hw = TROUGH_HW
t_top = FLOOR_Z
dy_t = t_hw - TROUGH_FLAT
dz_t = t_top - TROUGH_Z
r_t = (dy_t ** 2 + dz_t ** 2) / (2 * dz_t)
ang = math.asin(dy_t / r_t)
m_y = TROUGH_FLAT + r_t * math.sin(ang / 2)
m_z = TROUGH_Z + r_t * (1 - math.cos(ang / 2))
trough = (cq.Workplane("YZ")
          .moveTo(-t_hw, FLOOR_Z + 5)
          .lineTo(-t_hw, t_top)
          .threePointArc((-m_y, m_z), (-TROUGH_FLAT, TROUGH_Z))
          .lineTo(TROUGH_FLAT, TROUGH_Z)
          .threePointArc((m_y, m_z), (t_hw, t_top))
          .lineTo(t_hw, FLOOR_Z + 5)
          .close()
          .extrude(RAISED_X0 - LEDGE_X1).translate((LEDGE_X1, 0, 0)))
body = body.cut(trough)

# side tabs standing in the rims
for s in (1, -1):
    y0, y1 = (TAB_Y_IN, fw) if s > 0 else (-fw, -TAB_Y_IN)
    tab = box(TAB_X[0], TAB_X[1], y0, y1, TROUGH_Z - 1.0, RAISED_Z)
    tab = tab.faces(">Z").edges().chamfer(TAB_CH)
    body = body.union(tab)

# rounded bevels along the lower long edges of the floor
for s in (1, -1):
    b0, bm, b1, y_out = bottom_edge_profile(s)
    cut = (cq.Workplane("YZ")
           .moveTo(*b0).threePointArc(bm, b1)
           .lineTo(s * y_out, -0.05).lineTo(s * y_out, b0[1])
           .close()
           .extrude(PLATE_X0 - LEDGE_X1 - LEDGE_R2 + 0.5)
           .translate((LEDGE_X1 + LEDGE_R2, 0, 0)))
    body = body.cut(cut)

# the same rounded bevel wrapped around the concave ledge/floor corners
# (profile revolved 90 deg about the vertical axis of each concave blend)
_, c_mid, c_end, _ = bottom_edge_profile(1)
d_mid, d_end = fw - c_mid[0], fw - c_end[0]
corner_cut = (cq.Workplane("XZ")
              .moveTo(LEDGE_R2, BOT_CH_Z)
              .threePointArc((LEDGE_R2 + d_mid, c_mid[1]), (LEDGE_R2 + d_end, 0.0))
              .lineTo(LEDGE_R2 + d_end, -0.05)
              .lineTo(LEDGE_R2 - 0.05, -0.05)
              .lineTo(LEDGE_R2 - 0.05, BOT_CH_Z)
              .close()
              .revolve(90, (0, 0, 0), (0, 1, 0)))      # sector spanning +X .. +Y
for s in (1, -1):
    # rotate the sector so it spans from -X towards the floor side
    sector = corner_cut.rotate((0, 0, 0), (0, 0, 1), 90 if s < 0 else 180)
    sector = sector.translate((LEDGE_X1 + LEDGE_R2, s * (fw + LEDGE_R2), 0))
    sector = sector.intersect(box(LEDGE_X1, LEDGE_X1 + LEDGE_R2 + 0.01,
                                  -hw, hw, -1, BOT_CH_Z + 1))
    body = body.cut(sector)

# feet under the raised part
for fx in FOOT_X:
    for fy in FOOT_Y:
        body = body.union(cq.Workplane("XY").circle(FOOT_R).extrude(FOOT_H)
                          .translate((fx, fy, 0)))
for fx in FOOT_X:
    for fy in FOOT_Y:
        body = body.cut(cq.Workplane("XY").circle(POCKET_D / 2).extrude(POCKET_DEPTH)
                        .translate((fx, fy, 0)))
        body = body.cut(cq.Workplane("XY").add(
            cq.Solid.makeCone(POCKET_D / 2 + 0.6, POCKET_D / 2, 0.6,
                              pnt=cq.Vector(fx, fy, 0), dir=cq.Vector(0, 0, 1))))

# ---------------------------------------------------------------- floor cut-outs
for (x0, x1) in SLOT_X:
    body = body.cut(box(x0, x1, -SLOT_W / 2, SLOT_W / 2, -5, 30)
                    .edges("|Z").fillet(SLOT_R))
    for gy in GROOVE_Y:
        for s in (1, -1):
            body = body.cut(box(max(x0, LEDGE_X1 + 0.3), x1,
                                s * gy - GROOVE_W / 2, s * gy + GROOVE_W / 2,
                                TROUGH_Z - GROOVE_DEPTH, TROUGH_Z + 0.1))

for s in (1, -1):
    body = body.cut(cq.Workplane("XY").circle(CEN_HOLE_D / 2).extrude(40)
                    .translate((CEN_HOLE_X, s * CEN_HOLE_Y, -5)))
    body = body.cut(cq.Workplane("XY").add(
        cq.Solid.makeCone(CEN_CSK_D / 2, 0.0, CEN_CSK_D / 2,
                          pnt=cq.Vector(CEN_HOLE_X, s * CEN_HOLE_Y, 0),
                          dir=cq.Vector(0, 0, 1))))

# ledge through holes
for s in (1, -1):
    body = body.cut(cq.Workplane("XY").circle(LEDGE_HOLE_D / 2).extrude(40)
                    .translate((LEDGE_HOLE_X, s * LEDGE_HOLE_Y, -5)))

# ---------------------------------------------------------------- X holes (wall + plate)
for hz in HOLE_Z:
    for s in (1, -1):
        body = body.cut(cq.Workplane("YZ").circle(WALL_HOLE_D / 2).extrude(WALL_X1 + 5)
                        .translate((-2, s * HOLE_Y, hz)))
        body = body.cut(cq.Workplane("YZ").circle(HOLE_D / 2).extrude(10)
                        .translate((PLATE_X0 - 3, s * HOLE_Y, hz)))
        body = body.cut(cq.Workplane("XY").add(
            cq.Solid.makeCone(CSK_D / 2 + 0.05, CSK_D2 / 2, CSK_DEPTH + 0.05,
                              pnt=cq.Vector(PLATE_X1 + 0.05, s * HOLE_Y, hz),
                              dir=cq.Vector(-1, 0, 0))))
# counterbores on the back of the lower body (lower hole row)
for s in (1, -1):
    body = body.cut(cq.Workplane("YZ").circle(CB_D / 2).extrude(CB_DEPTH + 4)
                    .translate((COL_X_BOT - 4, s * HOLE_Y, HOLE_Z[0])))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
